import math
import cadquery as cq

# ---------------------------------------------------------------- dimensions (mm)
T = 6.85                 # base plate thickness
R_BIG = 36.0             # big round plate radius (centre at origin)
LOBE_X = -42.0           # left lobe centre x
R_LOBE = 32.9            # left lobe radius
CUT_R = 40.0             # shallow concave cut on the far left
CUT_DEPTH_X = -68.0      # x of the deepest point of that cut
CUT_Y = 0.7              # slight upward offset of that cut
TAB_X0 = 24.0            # tab block start x
TAB_X1 = 47.6            # tab block end x
TAB_HW = 20.6            # tab block half width
NECK_FILLET = 8.0        # plan-view fillet at the upper lobe / circle neck
TAB_FILLET = 5.0         # plan-view fillet where tab block meets the circle
EDGE_FILLET = 1.0        # rounding of the top outer edges of the round plate

# straight flat on the lower side of the lobe (between clip root and big circle)
FLAT_P0 = (-34.6, -31.7)
FLAT_P1 = (-25.1, -25.6)

LUG_XY = (-12.9, -29.7)  # small pin on its lug
LUG_R = 5.6
LUG_FILLET = 1.5
SMALL_PIN_D = 5.6
SMALL_PIN_TOP = 12.2

BAND_RI = 27.3           # raised C band inner radius
BAND_RO = 33.0           # raised C band outer radius
BAND_H = 4.9             # raised C band height above plate
BAND_A0 = -100.0         # band start angle (deg)
BAND_A1 = 125.0          # band end angle (deg)
BAND_FOOT_FILLET = 1.0

SLOT_Y = 12.1            # tab slot centre offset (+/-)
SLOT_CX = 41.0           # centre of slot end radius
SLOT_CB_W = 12.9         # counterbore width
SLOT_W = 7.2             # through slot width
SLOT_W_CX = 40.3         # centre of the through slot end radius
SLOT_FLOOR = 2.65        # counterbore floor height above bottom

HOLE_X = -57.0
HOLE_Y = 12.1
HOLE_D = 6.8
HOLE_CB_D = 10.6
HOLE_CB_DEPTH = 5.0

TALL_PIN_X = -42.2
TALL_PIN_D = 6.5
TALL_PIN_H = 9.95

HUB_D = 16.9
HUB_TOP = T + BAND_H
HUB_RECESS_D = 10.0
HUB_RECESS_DEPTH = 2.0
HUB_PIN_D = 6.6
HUB_PIN_TOP = HUB_TOP + 1.6

CLIP_ROOT = (-37.0, -33.1)     # where the clip leaves the lobe edge
CLIP_ANG = 22.4                # deg, clip runs from -Y rotated towards +X
CLIP_L = 15.5
CLIP_T = 4.0
CLIP_H = 15.5
CLIP_HOLE_U = 7.3              # hole position along the clip from its root
CLIP_HOLE_Z = 9.7
CLIP_HOLE_RY = 3.0             # oval jaw half width (along Y)
CLIP_HOLE_RZ = 2.35            # oval jaw half height
CLIP_SLOT_W = 3.4
CLIP_R_FREE = 3.5              # top corner radius at the free end
CLIP_R_ROOT = 2.0              # top corner radius at the root end


# ---------------------------------------------------------------- helpers
def cyl(x, y, r, z0, h):
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(r).extrude(h)


def is_vertical(e):
    p0 = e.startPoint()
    p1 = e.endPoint()
    return abs(p0.x - p1.x) < 1e-4 and abs(p0.y - p1.y) < 1e-4 and abs(p0.z - p1.z) > 1e-3


def at_z(e, z):
    return abs(e.startPoint().z - z) < 1e-4 and abs(e.endPoint().z - z) < 1e-4


def fillet_where(solid, radius, pred, fallbacks=()):
    edges = [e for e in solid.Edges() if pred(e)]
    if not edges:
        return solid
    for r in (radius,) + tuple(fallbacks):
        try:
            out = solid.fillet(r, edges)
            if out.isValid():
                return out
        except Exception:
            pass
    return solid


# ---------------------------------------------------------------- base plate outline
plate = cyl(0, 0, R_BIG, 0, T)

# left lobe: circle, shallow concave cut on the left, straight flat underneath
lobe = cyl(LOBE_X, 0, R_LOBE, 0, T)
lobe = lobe.cut(cyl(CUT_DEPTH_X - CUT_R, CUT_Y, CUT_R, -1, T + 2))
dx, dy = FLAT_P1[0] - FLAT_P0[0], FLAT_P1[1] - FLAT_P0[1]
ang = math.degrees(math.atan2(dy, dx))
cutter = (
    cq.Workplane("XY").workplane(offset=-1)
    .rect(80, 40).extrude(T + 2)
    .translate((0, -20, 0))
    .rotate((0, 0, 0), (0, 0, 1), ang)
    .translate((FLAT_P0[0], FLAT_P0[1], 0))
)
lobe = lobe.cut(cutter)
plate = plate.union(lobe)

plate = plate.union(
    cq.Workplane("XY").center((TAB_X0 + TAB_X1) / 2, 0)
    .rect(TAB_X1 - TAB_X0, 2 * TAB_HW).extrude(T)
)
plate = plate.union(cyl(LUG_XY[0], LUG_XY[1], LUG_R, 0, T))

solid = plate.val()

# plan-view concave fillets
solid = fillet_where(
    solid, NECK_FILLET,
    lambda e: is_vertical(e) and -30 < e.startPoint().x < -18 and e.startPoint().y > 20,
    (6.0, 4.0))
solid = fillet_where(
    solid, TAB_FILLET,
    lambda e: is_vertical(e) and 24 < e.startPoint().x < 33 and abs(e.startPoint().y) > 18,
    (4.0, 3.0))


def lug_pred(e):
    if not is_vertical(e):
        return False
    p = e.startPoint()
    d = math.hypot(p.x - LUG_XY[0], p.y - LUG_XY[1])
    # only the junction on the +X side is blended; the other one stays a sharp notch
    return abs(d - LUG_R) < 0.3 and abs(math.hypot(p.x, p.y) - R_BIG) < 0.3 and p.x > LUG_XY[0]


solid = fillet_where(solid, LUG_FILLET, lug_pred, (1.0,))
base = cq.Workplane("XY").add(solid)

# ---------------------------------------------------------------- stepped U slots in the tab block
for sy in (SLOT_Y, -SLOT_Y):
    Lcb = TAB_X1 + 2 - SLOT_CX
    Lth = TAB_X1 + 2 - SLOT_W_CX
    cb = (
        cq.Workplane("XY").workplane(offset=SLOT_FLOOR)
        .center(SLOT_CX + Lcb / 2, sy).rect(Lcb, SLOT_CB_W).extrude(T)
        .union(cyl(SLOT_CX, sy, SLOT_CB_W / 2, SLOT_FLOOR, T))
    )
    th = (
        cq.Workplane("XY").workplane(offset=-1)
        .center(SLOT_W_CX + Lth / 2, sy).rect(Lth, SLOT_W).extrude(T + 2)
        .union(cyl(SLOT_W_CX, sy, SLOT_W / 2, -1, T + 2))
    )
    base = base.cut(cb).cut(th)

# round the top edges of the round plate, lug, tab block and slot rims
solid = base.val()
solid = fillet_where(solid, EDGE_FILLET,
                     lambda e: at_z(e, T) and e.Center().x > -20,
                     (0.8, 0.6))
base = cq.Workplane("XY").add(solid)

# ---------------------------------------------------------------- raised C band
a0 = math.radians(BAND_A0)
a1 = math.radians(BAND_A1)
am = (a0 + a1) / 2
band = (
    cq.Workplane("XY").workplane(offset=T)
    .moveTo(BAND_RO * math.cos(a0), BAND_RO * math.sin(a0))
    .threePointArc((BAND_RO * math.cos(am), BAND_RO * math.sin(am)),
                   (BAND_RO * math.cos(a1), BAND_RO * math.sin(a1)))
    .lineTo(BAND_RI * math.cos(a1), BAND_RI * math.sin(a1))
    .threePointArc((BAND_RI * math.cos(am), BAND_RI * math.sin(am)),
                   (BAND_RI * math.cos(a0), BAND_RI * math.sin(a0)))
    .close()
    .extrude(BAND_H)
)
base = base.union(band)


def band_foot_pred(e):
    if not at_z(e, T):
        return False
    p0, p1 = e.startPoint(), e.endPoint()
    return abs(math.hypot(p0.x, p0.y) - BAND_RO) < 0.05 and abs(math.hypot(p1.x, p1.y) - BAND_RO) < 0.05


base = cq.Workplane("XY").add(fillet_where(base.val(), BAND_FOOT_FILLET, band_foot_pred, (0.7,)))

# ---------------------------------------------------------------- hub, pins
hub = cyl(0, 0, HUB_D / 2, T, HUB_TOP - T)
hub = hub.cut(cyl(0, 0, HUB_RECESS_D / 2, HUB_TOP - HUB_RECESS_DEPTH, 5))
hub = hub.union(cyl(0, 0, HUB_PIN_D / 2, HUB_TOP - HUB_RECESS_DEPTH,
                    HUB_PIN_TOP - HUB_TOP + HUB_RECESS_DEPTH))
base = base.union(hub)

base = base.union(cyl(TALL_PIN_X, 0, TALL_PIN_D / 2, T, TALL_PIN_H))
base = base.union(cyl(LUG_XY[0], LUG_XY[1], SMALL_PIN_D / 2, T, SMALL_PIN_TOP - T))

# ---------------------------------------------------------------- counterbored holes
for sy in (HOLE_Y, -HOLE_Y):
    base = base.cut(cyl(HOLE_X, sy, HOLE_D / 2, -1, T + 2))
    base = base.cut(cyl(HOLE_X, sy, HOLE_CB_D / 2, T - HOLE_CB_DEPTH, HOLE_CB_DEPTH + 1))

# ---------------------------------------------------------------- clip (upright hook with keyhole)
# drawn on the XZ plane: local x = distance along the clip from its root (0) to the free end (CLIP_L)
rf, rr = CLIP_R_FREE, CLIP_R_ROOT
c45 = math.cos(math.radians(45))
prof = (
    cq.Workplane("XZ")
    .moveTo(-1.5, 0)
    .lineTo(CLIP_L, 0)
    .lineTo(CLIP_L, CLIP_H - rf)
    .threePointArc((CLIP_L - rf + rf * c45, CLIP_H - rf + rf * c45), (CLIP_L - rf, CLIP_H))
    .lineTo(rr, CLIP_H)
    .threePointArc((rr - rr * c45, CLIP_H - rr + rr * c45), (0, CLIP_H - rr))
    .lineTo(0, T - 0.5)
    .lineTo(-1.5, T - 0.5)
    .close()
    .extrude(-CLIP_T)          # XZ normal is -Y: negative extrude goes towards +Y
)
clip = prof.translate((0, -CLIP_T / 2, 0))
clip = clip.rotate((0, 0, 0), (0, 0, 1), -(90 - CLIP_ANG))
clip = clip.translate((CLIP_ROOT[0], CLIP_ROOT[1], 0))

# keyhole (oval jaw + entry slot from the top), cut straight through along X
ca, sa = math.cos(math.radians(CLIP_ANG)), math.sin(math.radians(CLIP_ANG))
hx = CLIP_ROOT[0] + CLIP_HOLE_U * sa
hy = CLIP_ROOT[1] - CLIP_HOLE_U * ca
keyhole = (
    cq.Workplane("YZ").workplane(offset=hx - 8)
    .center(hy, CLIP_HOLE_Z).ellipse(CLIP_HOLE_RY, CLIP_HOLE_RZ).extrude(16)
    .union(
        cq.Workplane("YZ").workplane(offset=hx - 8)
        .center(hy, (CLIP_HOLE_Z + CLIP_H + 1) / 2)
        .rect(CLIP_SLOT_W, CLIP_H + 1 - CLIP_HOLE_Z).extrude(16)
    )
)
clip = clip.cut(keyhole)
base = base.union(clip)

result = base

VIEW = {"azimuth": 45, "elevation": 26}
